import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 400.0          # box width  (X)
L = 850.0          # box length (Y)
H = 362.0          # box height to lid top (Z)
LID_T = 5.0        # lid plate thickness
LID_OH = 1.0       # lid overhang
EDGE_R = 4.0       # vertical edge round of the body
FRONT_CH = 7.0     # chamfer under the front bottom lip
LIP_H = 10.5       # bottom lip height
LIP_OUT = 2.5      # lip projection in front of the front face
LIP_D = 30.0       # lip depth behind the front face
LIP_INSET = 2.0    # lip inset from the body sides

PAD_H = 23.0       # raised pad height on lid
PAD_X = 193.0      # pad half-length in X
PAD_R = 18.0       # pad end (X) top edge fillet
PAD_R2 = 1.5       # pad side (Y) edge fillet
PADS = [(-227.0, -135.0), (-105.0, -14.0), (16.0, 108.0), (117.0, 409.0)]
SLOT_W = 14.0
SLOT_D = 5.0
SLOT_HALF = 96.0   # narrow-pad slot half length (X)
SLOT_OFF = -8.0    # slot offset from pad centre (Y)
BIG_SLOT_X = 150.0
BIG_SLOT_Y = (208.0, 310.0)

KNOB_X = 135.0     # knob pocket centre |X|
POCKET_W = 63.0
POCKET_H = 50.0
POCKET_D = 35.0
KNOB_R = 25.0      # spindle max radius
KNOB_LEN = 58.0    # spindle length along X
KNOB_END_R = 15.0  # spindle end-rim radius
KNOB_PROJ = 15.0   # knob projection in front of the front face
KNOB_YC = KNOB_R - KNOB_PROJ   # spindle axis behind the front face
KNOB_DZ = 22.0     # knob axis below lid top
KNOB_SLOT_W = 4.0
KNOB_RIDGE = 1.5   # ridge height on the latch lever
KNOB_WING_ANG = 8.0

FIT_Y = -362.0     # side fittings
FIT_Z = 84.0
FIT_NECK_D, FIT_NECK_L = 15.0, 11.0
FIT_BODY_D, FIT_BODY_L = 27.0, 43.5
FIT_FL_SPAN, FIT_FL_W, FIT_FL_T = 46.0, 12.0, 9.0

EXT_D = 99.0       # rear extension depth (Y)
EXT_INSET = 3.0    # inset from body sides
EXT_Z0 = 9.0       # rear extension bottom
EXT_SPLIT_X = -16.0  # x where the sloped part begins
SLOPE_Y0 = 8.0     # slope start behind body back face
SLOPE_Z_END = 210.0  # height of sloped part at the rear face
EXT_RB = 8.0      # rear extension bottom edge round
EXT_RV = 4.0      # rear extension vertical edge round
EXT_RT = 5.0      # rear extension top edge round

BOT_REC_D = 4.0    # recessed panels on the underside
BOT_FRONT_X = 166.0
BOT_FRONT_Y = (-222.0, 68.0)
BOT_LAND = 8.0
BOT_GAP = 6.0
BOT_BIG_X = 168.0
BOT_BIG_Y = (90.0, 405.0)

y0, y1 = -L / 2.0, L / 2.0

# ---------------- main body ----------------
body = (cq.Workplane("XY")
        .box(W, L, H - LID_T, centered=(True, True, False))
        .edges("|Z").fillet(EDGE_R))

# bottom tray lip, slightly proud of the front face, chamfered underneath
lip = (cq.Workplane("XY")
       .box(W - 2 * LIP_INSET, LIP_D + LIP_OUT, LIP_H, centered=(True, False, False))
       .translate((0, y0 - LIP_OUT, 0))
       .faces("<Z").edges("<Y").chamfer(FRONT_CH)
       .edges("|Z and <Y").fillet(1.5))
body = body.union(lip)

lid = (cq.Workplane("XY").workplane(offset=H - LID_T)
       .center(0, -LID_OH / 2.0)
       .box(W + 2 * LID_OH, L + LID_OH, LID_T, centered=(True, True, False))
       .edges("|Z").fillet(EDGE_R))
body = body.union(lid)

# ---------------- raised pads on the lid ----------------
for (ya, yb) in PADS:
    pad = (cq.Workplane("XY")
           .box(2 * PAD_X, yb - ya, PAD_H + 1.0, centered=(True, True, False))
           .edges("|Y and >Z").fillet(PAD_R))
    pad = pad.faces("<Y or >Y").edges("not(<Z)").fillet(PAD_R2)
    pad = pad.translate((0, (ya + yb) / 2.0, H - 1.0))
    body = body.union(pad)

# slots in pad tops
for (ya, yb) in PADS[:3]:
    yc = (ya + yb) / 2.0 + SLOT_OFF
    slot = (cq.Workplane("XY").workplane(offset=H + PAD_H - SLOT_D)
            .center(0, yc)
            .rect(2 * SLOT_HALF, SLOT_W)
            .extrude(SLOT_D + 1))
    body = body.cut(slot)
big_slot = (cq.Workplane("XY").workplane(offset=H + PAD_H - SLOT_D)
            .center(BIG_SLOT_X, sum(BIG_SLOT_Y) / 2.0)
            .rect(SLOT_W, BIG_SLOT_Y[1] - BIG_SLOT_Y[0])
            .extrude(SLOT_D + 1))
body = body.cut(big_slot)

# ---------------- knob pockets and knobs ----------------
def make_knob():
    """Spindle-shaped latch lever, axis along X, front face plane at y=0."""
    half = KNOB_LEN / 2.0
    prof = (cq.Workplane("XY").moveTo(-half, 0).lineTo(-half, KNOB_END_R)
            .threePointArc((0, KNOB_R), (half, KNOB_END_R)).lineTo(half, 0).close())
    k = prof.revolve(360, (-half, 0, 0), (half, 0, 0))
    k = k.translate((0, KNOB_YC, 0))
    shank = (cq.Workplane("XZ").workplane(offset=-KNOB_YC)
             .circle(KNOB_R * 0.5).extrude(-(POCKET_D + 2 - KNOB_YC)))
    k = k.union(shank)
    # raised ridge following the spindle contour along its front
    rc2 = KNOB_R + KNOB_RIDGE
    prof2 = (cq.Workplane("XY").moveTo(-half, 0).lineTo(-half, KNOB_END_R + KNOB_RIDGE)
             .threePointArc((0, rc2), (half, KNOB_END_R + KNOB_RIDGE)).lineTo(half, 0).close())
    outer = prof2.revolve(360, (-half, 0, 0), (half, 0, 0)).translate((0, KNOB_YC, 0))
    fin = (cq.Workplane("XY")
           .box(KNOB_LEN - 0.5, rc2, KNOB_SLOT_W, centered=(True, False, True))
           .translate((0, KNOB_YC - rc2, 0)))
    ridge = fin.intersect(outer).rotate((0, 0, 0), (0, 1, 0), KNOB_WING_ANG)
    k = k.union(ridge)
    for ex in (-1, 1):
        ear = (cq.Workplane("YZ").workplane(offset=ex * (half - 8.0))
               .center(KNOB_YC + 2.0, 0).circle(KNOB_R * 0.45).extrude(ex * 4.0))
        k = k.union(ear)
    return k

for sx in (-1, 1):
    xc = sx * KNOB_X
    pocket = (cq.Workplane("XY")
              .box(POCKET_W, POCKET_D + 10, POCKET_H + 10, centered=(True, False, False))
              .translate((xc, y0 - 10 - LID_OH, H - POCKET_H)))
    body = body.cut(pocket)
    knob = make_knob().translate((xc, y0, H - KNOB_DZ))
    body = body.union(knob)

# ---------------- side fittings ----------------
for sx in (-1, 1):
    xw = sx * W / 2.0
    neck = (cq.Workplane("YZ").workplane(offset=xw - sx * 1.0)
            .center(FIT_Y, FIT_Z).circle(FIT_NECK_D / 2.0).extrude(sx * (FIT_NECK_L + 1.0)))
    bodyc = (cq.Workplane("YZ").workplane(offset=xw + sx * FIT_NECK_L)
             .center(FIT_Y, FIT_Z).circle(FIT_BODY_D / 2.0).extrude(sx * FIT_BODY_L))
    xf = xw + sx * (FIT_NECK_L + FIT_BODY_L)
    fl = (cq.Workplane("YZ").workplane(offset=xf)
          .center(FIT_Y, FIT_Z)
          .slot2D(FIT_FL_SPAN, FIT_FL_W, 0).extrude(sx * FIT_FL_T))
    fl2 = (cq.Workplane("YZ").workplane(offset=xf)
           .center(FIT_Y, FIT_Z)
           .slot2D(FIT_FL_SPAN, FIT_FL_W, 90).extrude(sx * FIT_FL_T))
    hub = (cq.Workplane("YZ").workplane(offset=xf)
           .center(FIT_Y, FIT_Z).circle(FIT_BODY_D / 2.0 - 2).extrude(sx * (FIT_FL_T + 3)))
    fit = neck.union(bodyc).union(fl).union(fl2).union(hub)
    hole_r = (FIT_FL_SPAN - FIT_FL_W) / 2.0
    holes = (cq.Workplane("YZ").workplane(offset=xf - 2 * sx)
             .pushPoints([(FIT_Y + hole_r, FIT_Z), (FIT_Y - hole_r, FIT_Z),
                          (FIT_Y, FIT_Z + hole_r), (FIT_Y, FIT_Z - hole_r)])
             .circle(2.2).extrude(sx * (FIT_FL_T + 4)))
    fit = fit.cut(holes)
    body = body.union(fit)

# ---------------- rear extension ----------------
ext_w = W - 2 * EXT_INSET
ext = (cq.Workplane("XY")
       .box(ext_w, EXT_D + 2, H - EXT_Z0, centered=(True, False, False))
       .translate((0, y1 - 2, EXT_Z0)))
ext = ext.faces("<Z").edges("not <Y").fillet(EXT_RB)
ext = ext.edges("|Z and >Y").fillet(EXT_RV)
ext = ext.faces(">Z").edges("not <Y").fillet(EXT_RT)
# slope cut on the +X portion: plane through the top edge just behind the
# body (y1 + SLOPE_Y0, H) and the rear face at height SLOPE_Z_END
run = 20.0
drop = (H - SLOPE_Z_END) / (EXT_D - SLOPE_Y0)
wedge = (cq.Workplane("YZ").workplane(offset=EXT_SPLIT_X)
         .polyline([(y1 + SLOPE_Y0, H + run),
                    (y1 + EXT_D + run, H + run),
                    (y1 + EXT_D + run, SLOPE_Z_END - drop * run),
                    (y1 + SLOPE_Y0, H)]).close()
         .extrude(W))
ext = ext.cut(wedge)
body = body.union(ext)

# ---------------- underside recessed panels ----------------
# front group: shallow outer recess holding three deeper strips
fg_y0, fg_y1 = BOT_FRONT_Y
rec1 = (cq.Workplane("XY").center(0, (fg_y0 + fg_y1) / 2.0)
        .rect(2 * BOT_FRONT_X, fg_y1 - fg_y0).extrude(BOT_REC_D))
body = body.cut(rec1)
strip_len = (fg_y1 - fg_y0 - 2 * BOT_LAND - 2 * BOT_GAP) / 3.0
for i in range(3):
    sy0 = fg_y0 + BOT_LAND + i * (strip_len + BOT_GAP)
    strip = (cq.Workplane("XY")
             .center(-BOT_LAND / 2.0, sy0 + strip_len / 2.0)
             .rect(2 * BOT_FRONT_X - 3 * BOT_LAND, strip_len)
             .extrude(2 * BOT_REC_D))
    body = body.cut(strip)
bg_y0, bg_y1 = BOT_BIG_Y
rec2 = (cq.Workplane("XY").center(0, (bg_y0 + bg_y1) / 2.0)
        .rect(2 * BOT_BIG_X, bg_y1 - bg_y0).extrude(BOT_REC_D))
body = body.cut(rec2)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
